import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 120.0          # outer length (X)
W = 60.0           # outer width (Y)
H_BODY = 16.4      # height of the main body up to the outer ledge
R_OUT = 5.5        # outer vertical corner radius
T_WALL = 2.55      # side wall thickness
R_IN = 3.2         # inner vertical corner radius of the cavity
T_FLOOR = 2.3      # floor thickness
FLOOR_FIL = 2.0    # inner floor-to-wall fillet radius

# tongue (lip) on the inner part of the wall top, for the mating lid
LEDGE = 1.4        # width of the outer ledge (tongue set back from the outer face)
LIP_H = 1.4        # tongue height above the ledge
LIP_CHAMFER = 0.35 # lead-in chamfer on the outer top edge of the tongue

# screw bosses (4x) with flared foot, countersunk from below
BOSS_D = 8.5
BOSS_H = 3.8       # above the floor
BOSS_FIL = 2.5     # flare radius at the boss foot
HOLE_D = 4.4
CSK_D = 10.0       # 90 deg countersink on the underside
BOSS_X = (-46.6, 50.6)
BOSS_Y = (-18.05, 20.65)

# rectangular port through the front (-Y) wall
PORT_W = 17.8
PORT_H = 10.0
PORT_X = 38.15     # port centre x
PORT_Z0 = 4.3      # port sill height above the base

# ---------------- main shell ----------------
outer = (
    cq.Workplane("XY")
    .rect(L, W)
    .extrude(H_BODY)
    .edges("|Z")
    .fillet(R_OUT)
)

lip = (
    cq.Workplane("XY")
    .workplane(offset=H_BODY)
    .rect(L - 2 * LEDGE, W - 2 * LEDGE)
    .extrude(LIP_H)
    .edges("|Z")
    .fillet(R_OUT - LEDGE)
    .faces(">Z")
    .edges()
    .chamfer(LIP_CHAMFER)
)
body = outer.union(lip)

cavity = (
    cq.Workplane("XY")
    .workplane(offset=T_FLOOR)
    .rect(L - 2 * T_WALL, W - 2 * T_WALL)
    .extrude(H_BODY + LIP_H)
    .edges("|Z")
    .fillet(R_IN)
    .faces("<Z")
    .edges()
    .fillet(FLOOR_FIL)
)
body = body.cut(cavity)

# ---------------- bosses ----------------
rb, rf, hb = BOSS_D / 2.0, BOSS_FIL, BOSS_H
k = 1.0 - math.sqrt(0.5)
boss_profile = (
    cq.Workplane("XZ")
    .moveTo(0, -0.8)
    .lineTo(rb + rf, -0.8)
    .lineTo(rb + rf, 0)
    .threePointArc((rb + rf * k, rf * k), (rb, rf))
    .lineTo(rb, hb)
    .lineTo(0, hb)
    .close()
)
boss = boss_profile.revolve(360, (0, 0, 0), (0, 1, 0))

pts = [(x, y) for x in BOSS_X for y in BOSS_Y]
for (x, y) in pts:
    body = body.union(boss.translate((x, y, T_FLOOR)))

# through holes + countersinks from the underside
for (x, y) in pts:
    hole = (
        cq.Workplane("XY")
        .center(x, y)
        .circle(HOLE_D / 2.0)
        .extrude(T_FLOOR + hb + 2.0)
        .translate((0, 0, -1.0))
    )
    csk = cq.Solid.makeCone(CSK_D / 2.0 + 1.0, 0.0, CSK_D / 2.0 + 1.0,
                            cq.Vector(x, y, -1.0))
    body = body.cut(hole).cut(cq.Workplane("XY").add(csk))

# ---------------- port in the front wall ----------------
port = (
    cq.Workplane("XY")
    .box(PORT_W, 2.0 * T_WALL + 2.0, PORT_H)
    .translate((PORT_X, -W / 2.0, PORT_Z0 + PORT_H / 2.0))
)
body = body.cut(port)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
